import cadquery as cq

# ---------------------------------------------------------------------------
# Square plate with a spherical seat cut through it.
# The plate stands upright in the XZ plane (thickness along Y).  A sphere whose
# centre lies on the centre of the FRONT face (y = -T/2) is subtracted, so the
# opening is D_SPHERE wide at the front face and narrows (curved wall) to
#   D_back = 2*sqrt(R^2 - T^2)  at the back face.
# ---------------------------------------------------------------------------

# Driving dimensions (mm)
W = 100.0          # plate width  (X)
H = 100.0          # plate height (Z)
T = 19.5           # plate thickness (Y)
D_SPHERE = 91.2    # spherical seat diameter = opening diameter at the front face

R = D_SPHERE / 2.0
Y_FRONT = -T / 2.0

# Plate body, centred on the origin
plate = cq.Workplane("XZ").rect(W, H).extrude(T / 2.0, both=True)

# Spherical cutter centred on the front face.  Its polar axis lies in the
# front-face plane so the surface seam coincides with the front edge of the
# opening instead of running across the curved wall.
sphere = cq.Solid.makeSphere(
    R,
    pnt=cq.Vector(0, Y_FRONT, 0),
    dir=cq.Vector(-1, 0, 0),
    angleDegrees1=-90,
    angleDegrees2=90,
)

result = plate.cut(cq.Workplane("XY").add(sphere))

VIEW = {"azimuth": 45, "elevation": 26}
